import math
import cadquery as cq

# ---------------------------------------------------------------
# Servo C-bracket with a thick triangular mounting block
# Axis of the two round flanges = Z axis (X=0, Y=0)
# ---------------------------------------------------------------
H = 100.0            # overall height
ZM = H / 2.0         # mid plane (part is nearly symmetric about it)
T_PLATE = 7.4        # top / bottom plate thickness
T_DISC_T = 6.9       # disc under the top plate
T_DISC_B = 5.6       # disc above the bottom plate
R_PLATE = 25.5       # round part of the plates
R_DISC = 21.35       # disc above the bottom plate
R_DISC_T = 20.0      # disc under the top plate
Y_FLAT = -13.0       # flat truncation of the plates (-Y side)
R_CORNER = 4.0       # corner radius plate flat / left arc
R_CORNER_R = 5.0     # corner radius plate flat / circle (+X side)
BIG_R = 286.0        # convex arc on the -X side of the plates (plan), near the corner
BIG_Y_T = 43.0       # where that arc is tangent to X_OUT
# smooth -X outline (plan) of spine + block, from the plate corner to the tip
LEFT_PTS = [(-23.5, 5.0), (-25.25, 22.0), (-26.0, 40.0), (-25.05, 60.0),
            (-20.2, 80.0), (-11.3, 100.0), (-3.5, 112.0)]
LEFT_T_END = (0.59, 0.81)
SLOT_W = 24.0        # U-slot width in the plates
R_JOIN = 8.0         # concave fillet plate circle -> spine (plan)
R_HORN = 11.8        # raised horn disc inside the top slot
H_HORN = 3.8

# C-arm (spine)
X_OUT = -26.0        # outer (-X) face of spine
X_IN = -10.9         # +X face of spine
Y_IN_A = 28.0        # inner face of C at X_OUT
ELL_A = (10.6, 19.5) # elliptical inner blend (Y, Z semi axes) at X_OUT
Y_IN_B = 40.3        # inner face of C at X_IN
ELL_B = (15.2, 17.5) # elliptical inner blend at X_IN
Y_OUT = 48.7         # outer face of C
SH_A = 24.0          # start of the shoulder on the top face
SH_PTS = [(31.7, 97.5), (42.7, 90.6)]  # points on the shoulder curve (Y,Z)
SH_END = (48.7, 87.0)  # end of shoulder line (= start of triangle edge)
R_SPINE_EDGE = 2.5   # round on the outer inner-edge of the spine

# triangular block
Y_TIP = 105.5
R_TIP = 9.0
FRONT_P = (-7.0, 49.4)    # front face base point (X,Y)
FRONT_SLOPE = 0.39        # dX/dY of the front face
CH_TOP = 6.4              # long chamfer on the front outline: width on top face
CH_FRONT = 1.2            # ... and depth on the front face
R_BASE_EDGE = 1.5         # round on the vertical base edge of the front face

# cutout in triangle (YZ profile)
CUT_Z_HALF = 14.7
CUT_Y_TIP = 84.2
CUT_R = 2.6

# holes in triangle (Y, +-dZ from mid plane)
HOLES_YZ = [(65.9, 16.7), (78.8, 8.1), (91.1, 0.0)]
D_HOLE = 3.0
D_CB = 6.2
CB_DEPTH = 2.8

# flange holes
BC_R_T = 16.3
BC_R_B = 16.2
D_FH = 3.1
ANG_T = 29.0        # angular offset of the top hole circle
ANG_B = 35.0        # angular offset of the bottom hole circle
N_RING = 12         # small hole ring through the top disc
R_RING = 16.8
D_RING = 2.0
RING_ANG0 = 0.0


def mz(p):
    """mirror a (Y,Z) point about the mid plane"""
    return (p[0], H - p[1])


# ---------------- triangle edge (tangent to the tip circle) ----------------
yc_tip = Y_TIP - R_TIP
py, pz = SH_END
d_pc = math.hypot(yc_tip - py, ZM - pz)
ang = math.atan2(ZM - pz, yc_tip - py) + math.asin(R_TIP / d_pc)
ux, uz = math.cos(ang), math.sin(ang)
tp_up = (yc_tip - R_TIP * uz, ZM + R_TIP * ux)
tp_dn = mz(tp_up)
slope_tri = uz / ux


def z_top(y):
    return pz + slope_tri * (y - py)


# ---------------- shoulder of the C (YZ) ----------------
# smooth S-shaped shoulder from the plate top into the triangle edge


def outer_boundary(wp, y0):
    """top line -> shoulder -> (outer face) -> lower shoulder -> bottom line"""
    pts_up = list(SH_PTS) + [SH_END]
    pts_dn = [mz(p) for p in reversed(SH_PTS)] + [(SH_A, 0.0)]
    return (
        wp.moveTo(y0, H)
        .lineTo(SH_A, H)
        .spline(pts_up, tangents=[(1.0, 0.0), (1.0, slope_tri)], includeCurrent=True)
        .lineTo(*mz(SH_END))
        .spline(pts_dn, tangents=[(-1.0, slope_tri), (-1.0, 0.0)], includeCurrent=True)
        .lineTo(y0, 0.0)
    )


def c_profile(wp, y_in, ea, eb, top_line_y0=0.0):
    """closed C profile on a YZ workplane.
    y_in: inner face of the C, (ea, eb): semi axes of the elliptical
    inner blends towards the plates."""
    return (
        outer_boundary(wp, top_line_y0)
        .lineTo(top_line_y0, T_PLATE)
        .lineTo(y_in - ea, T_PLATE)
        .ellipseArc(ea, eb, angle1=270, angle2=360, startAtCurrent=True)
        .lineTo(y_in, H - T_PLATE - eb)
        .ellipseArc(ea, eb, angle1=0, angle2=90, startAtCurrent=True)
        .lineTo(top_line_y0, H - T_PLATE)
        .close()
    )


# spine: ruled loft between two C profiles -> inner face is inclined
# (wider opening on the +X side), giving the characteristic bevelled look
# the loft starts a little outside X_OUT; the -X face is then cut by the
# smooth plan outline (CLIP) shared with plates and block
X_L0 = X_OUT - 1.0
fr = (X_OUT - X_L0) / (X_IN - X_OUT)
y_in_0 = Y_IN_A - (Y_IN_B - Y_IN_A) * fr
ell_0 = (ELL_A[0] - (ELL_B[0] - ELL_A[0]) * fr, ELL_A[1] - (ELL_B[1] - ELL_A[1]) * fr)
arm_wp = c_profile(cq.Workplane("YZ", origin=(X_L0, 0, 0)), y_in_0, *ell_0)
arm = c_profile(arm_wp.workplane(offset=X_IN - X_L0), Y_IN_B, *ELL_B).loft(ruled=True)

# ---------------- plates ----------------

# envelope that trims the plates to the shoulder curve
env = outer_boundary(cq.Workplane("YZ", origin=(-60, 0, 0)), -40.0).close().extrude(120)


# big convex arc forming the -X side of the plates (tangent to the spine face)
BIG_C = (X_OUT + BIG_R, BIG_Y_T)


def big_arc_x(y):
    return BIG_C[0] - math.sqrt(BIG_R ** 2 - (y - BIG_C[1]) ** 2)


def left_corner():
    """fillet between the big arc and the flat (plan)"""
    v = (big_arc_x(Y_FLAT), Y_FLAT)
    rv = ((v[0] - BIG_C[0]) / BIG_R, (v[1] - BIG_C[1]) / BIG_R)
    d_arc = (rv[1], -rv[0])           # tangent pointing +Y
    if d_arc[1] < 0:
        d_arc = (-d_arc[0], -d_arc[1])
    th = math.acos(d_arc[0])          # angle between +X and arc tangent
    L = R_CORNER / math.tan(th / 2)
    p_flat = (v[0] + L, Y_FLAT)
    p_arc = (v[0] + d_arc[0] * L, v[1] + d_arc[1] * L)
    bis = (1 + d_arc[0], d_arc[1])
    nb = math.hypot(*bis)
    dm = R_CORNER / math.sin(th / 2) - R_CORNER
    p_mid = (v[0] + bis[0] / nb * dm, v[1] + bis[1] / nb * dm)
    return p_arc, p_mid, p_flat


def plan_clip(z0, h):
    """region right of the smooth -X outline of plates, spine and block
    (corner round at the plate flat + one spline up to the block tip)"""
    p_arc, p_mid, p_flat = left_corner()
    r = (p_arc[0] - BIG_C[0], p_arc[1] - BIG_C[1])
    t0 = (-r[1], r[0]) if r[0] > 0 else (r[1], -r[0])
    if t0[1] < 0:
        t0 = (-t0[0], -t0[1])
    y_top = LEFT_PTS[-1][1]
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(80, Y_FLAT - 30)
        .lineTo(p_flat[0], Y_FLAT - 30)
        .lineTo(*p_flat)
        .threePointArc(p_mid, p_arc)
        .spline(LEFT_PTS, tangents=[t0, LEFT_T_END], includeCurrent=True)
        .lineTo(80, y_top)
        .close()
        .extrude(h)
    )


CLIP = plan_clip(-2.0, H + 4.0)


def plate(z0):
    xc = math.sqrt(R_PLATE ** 2 - Y_FLAT ** 2)
    # concave join fillet between circle and spine +X face
    yf = math.sqrt((R_PLATE + R_JOIN) ** 2 - (X_IN + R_JOIN) ** 2)
    fc = (X_IN + R_JOIN, yf)
    k = R_PLATE / (R_PLATE + R_JOIN)
    t_circ = (fc[0] * k, fc[1] * k)
    a0 = math.atan2(t_circ[1] - fc[1], t_circ[0] - fc[0])
    a1 = -math.pi
    am = (a0 + a1) / 2
    f_mid = (fc[0] + R_JOIN * math.cos(am), fc[1] + R_JOIN * math.sin(am))
    # round corner between the flat and the circle (+X side)
    rc = R_CORNER_R
    cc = (math.sqrt((R_PLATE - rc) ** 2 - (Y_FLAT + rc) ** 2), Y_FLAT + rc)
    kc = R_PLATE / (R_PLATE - rc)
    c_t = (cc[0] * kc, cc[1] * kc)
    dvx, dvy = xc - cc[0], Y_FLAT - cc[1]
    dn = math.hypot(dvx, dvy)
    c_m = (cc[0] + rc * dvx / dn, cc[1] + rc * dvy / dn)
    a_c0 = math.atan2(c_t[1], c_t[0])
    a_c1 = math.atan2(t_circ[1], t_circ[0])
    a_cm = (a_c0 + a_c1) / 2
    c_mid = (R_PLATE * math.cos(a_cm), R_PLATE * math.sin(a_cm))
    w = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(X_IN, 40.0)
        .lineTo(X_OUT - 5.0, 40.0)
        .lineTo(X_OUT - 5.0, Y_FLAT)
        .lineTo(cc[0], Y_FLAT)
        .threePointArc(c_m, c_t)
        .threePointArc(c_mid, t_circ)
        .threePointArc(f_mid, (X_IN, fc[1]))
        .close()
        .extrude(T_PLATE)
    )
    slot = (
        cq.Workplane("XY", origin=(0, 0, z0 - 1))
        .moveTo(-SLOT_W / 2, Y_FLAT - 5)
        .lineTo(-SLOT_W / 2, 0)
        .threePointArc((0, SLOT_W / 2), (SLOT_W / 2, 0))
        .lineTo(SLOT_W / 2, Y_FLAT - 5)
        .close()
        .extrude(T_PLATE + 2)
    )
    return w.cut(slot).intersect(env).intersect(CLIP)


arm = arm.intersect(CLIP)
try:
    arm = arm.edges(cq.selectors.BoxSelector((X_OUT - 0.6, 12.0, 3.0), (X_OUT + 0.6, 34.0, H - 3.0))).fillet(R_SPINE_EDGE)
except Exception:
    pass
top_plate = plate(H - T_PLATE)
bot_plate = plate(0.0)

# discs
top_disc = cq.Workplane("XY", origin=(0, 0, H - T_PLATE - T_DISC_T)).circle(R_DISC_T).extrude(T_DISC_T)
bot_disc = cq.Workplane("XY", origin=(0, 0, T_PLATE)).circle(R_DISC).extrude(T_DISC_B)
horn = cq.Workplane("XY", origin=(0, 0, H - T_PLATE)).circle(R_HORN).extrude(H_HORN)

# bearing boss on the bottom disc
Z_BOSS0 = T_PLATE + T_DISC_B
boss = (
    cq.Workplane("XY", origin=(0, 0, Z_BOSS0)).circle(6.7).extrude(7.5)
    .union(cq.Workplane("XY", origin=(0, 0, Z_BOSS0)).circle(7.2).extrude(0.9))
)

# ---------------- triangular block ----------------
side = (
    cq.Workplane("YZ", origin=(-40, 0, 0))
    .moveTo(40.0, z_top(40.0))
    .lineTo(*tp_up)
    .threePointArc((Y_TIP, ZM), tp_dn)
    .lineTo(40.0, H - z_top(40.0))
    .close()
    .extrude(80)
)


def x_front(y):
    return FRONT_P[0] + FRONT_SLOPE * (y - FRONT_P[1])


phi = math.atan(FRONT_SLOPE)
y_end = 112.0
# base end face: perpendicular to the front face, from FRONT_P into the spine
x_base = X_IN - 1.0
t_base = (FRONT_P[0] - x_base) / math.cos(phi)
y_base = FRONT_P[1] + t_base * math.sin(phi)
plan = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .moveTo(X_OUT - 5.0, Y_OUT)
    .lineTo(X_OUT - 5.0, y_end)
    .lineTo(x_front(y_end), y_end)
    .lineTo(*FRONT_P)
    .lineTo(x_base, y_base)
    .lineTo(x_base, Y_OUT)
    .close()
    .extrude(H + 2)
)
block = side.intersect(plan).intersect(CLIP)


def on_front_plane(v, tol=1e-3):
    return abs((v.x - FRONT_P[0]) * math.cos(phi) - (v.y - FRONT_P[1]) * math.sin(phi)) < tol


# round the outer edges of the front (mounting) face
front_edges = []
base_edges = []
for e in block.val().Edges():
    pts = [e.startPoint(), e.endPoint(), e.positionAt(0.5)]
    if all(on_front_plane(p) for p in pts):
        if abs(pts[0].z - pts[1].z) > H * 0.5 and abs(pts[0].y - pts[1].y) < 1e-3:
            base_edges.append(e)       # vertical base edge
        else:
            front_edges.append(e)
# long shallow chamfer around the outline of the front face
# (CH_TOP measured on the top/bottom faces, CH_FRONT on the front face)
try:
    block = block.newObject(front_edges).chamfer(CH_TOP, CH_FRONT)
except Exception:
    pass
# small round on the vertical base edge of the front face
try:
    bsel = [e for e in block.val().Edges()
            if abs(e.startPoint().z - e.endPoint().z) > 20
            and on_front_plane(e.startPoint()) and on_front_plane(e.endPoint())]
    block = block.newObject(bsel).fillet(R_BASE_EDGE)
except Exception:
    pass

body = (
    arm.union(top_plate)
    .union(bot_plate)
    .union(top_disc)
    .union(bot_disc)
    .union(horn)
    .union(boss)
    .union(block)
)

# ---------------- cutout in triangle ----------------
cut_sk = (
    cq.Sketch()
    .polygon([(Y_OUT, ZM + CUT_Z_HALF), (CUT_Y_TIP, ZM), (Y_OUT, ZM - CUT_Z_HALF), (Y_OUT, ZM + CUT_Z_HALF)])
    .vertices()
    .fillet(CUT_R)
)
cut = cq.Workplane("YZ", origin=(-40, 0, 0)).placeSketch(cut_sk).extrude(80)
body = body.cut(cut)

# ---------------- counterbored holes in triangle (normal to front face) ----------------
n_front = cq.Vector(math.cos(phi), -math.sin(phi), 0)
for (hy, dzh) in HOLES_YZ:
    for s in ([1, -1] if dzh > 0 else [1]):
        hz = ZM + s * dzh
        p = cq.Vector(x_front(hy), hy, hz)
        thru = cq.Solid.makeCylinder(D_HOLE / 2, 60, p + n_front * 5, -n_front)
        cb = cq.Solid.makeCylinder(D_CB / 2, CB_DEPTH + 5, p + n_front * 5, -n_front)
        body = body.cut(cq.Workplane().add(thru)).cut(cq.Workplane().add(cb))

# ---------------- flange holes ----------------
# top plate: 8-hole circle, 6 of them in the plate (two fall into the slot)
for k in range(8):
    ad = ANG_T + 45 * k
    x = BC_R_T * math.cos(math.radians(ad))
    y = BC_R_T * math.sin(math.radians(ad))
    if abs(x) < SLOT_W / 2 and y < 0:
        continue                      # these fall into the slot
    c = cq.Solid.makeCylinder(D_FH / 2, T_PLATE + 2, cq.Vector(x, y, H - T_PLATE - 1), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane().add(c))
# ring of small holes through the top disc (three show inside the slot)
for k in range(N_RING):
    ad = RING_ANG0 + 360.0 / N_RING * k
    x = R_RING * math.cos(math.radians(ad))
    y = R_RING * math.sin(math.radians(ad))
    c = cq.Solid.makeCylinder(D_RING / 2, T_DISC_T + 2, cq.Vector(x, y, H - T_PLATE - T_DISC_T - 1), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane().add(c))
# shallow recess under the top disc
rec = cq.Solid.makeCylinder(14.5, 0.8, cq.Vector(0, 0, H - T_PLATE - T_DISC_T - 0.01), cq.Vector(0, 0, 1))
body = body.cut(cq.Workplane().add(rec))

# bottom disc: 8 holes through disc and plate
for k in range(8):
    ad = ANG_B + 45 * k
    x = BC_R_B * math.cos(math.radians(ad))
    y = BC_R_B * math.sin(math.radians(ad))
    c = cq.Solid.makeCylinder(D_FH / 2, T_PLATE + T_DISC_B + 2, cq.Vector(x, y, -1), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane().add(c))

# bore through the boss
bore = cq.Solid.makeCylinder(4.9, 30, cq.Vector(0, 0, -1), cq.Vector(0, 0, 1))
body = body.cut(cq.Workplane().add(bore))

# horn: centre hole + small holes
ch = cq.Solid.makeCylinder(2.4, 20, cq.Vector(0, 0, H - 15), cq.Vector(0, 0, 1))
body = body.cut(cq.Workplane().add(ch))
for k in range(4):
    ad = 83 + 90 * k
    x = 10.0 * math.cos(math.radians(ad))
    y = 10.0 * math.sin(math.radians(ad))
    c = cq.Solid.makeCylinder(0.8, T_DISC_T + H_HORN + 2, cq.Vector(x, y, H - T_PLATE - T_DISC_T - 1), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane().add(c))
for ad in (150, -30):
    x = 6.5 * math.cos(math.radians(ad))
    y = 6.5 * math.sin(math.radians(ad))
    c = cq.Solid.makeCylinder(0.9, 15, cq.Vector(x, y, H - 14), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane().add(c))

result = body
